"""Flanged split-clamp shaft hub.

A round mounting flange with an 8-hole bolt circle carries a cylindrical
hub with a blind shaft bore.  The +X half of the hub is freed by a thin
horizontal relief slot and split by a vertical slit, forming a clamp
that is closed by a tangential cap screw (counterbored on the +Y side,
hex nut captured in a square access pocket on the -Y side).
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 125.0          # flange outer diameter
FLANGE_T = 8.0            # flange thickness
HUB_D = 80.0              # clamp hub outer diameter
HUB_H = 37.5              # hub height above the flange
BORE_D = 40.0             # shaft bore diameter (blind)
BORE_BOTTOM_Z = FLANGE_T  # bore stops at the flange (solid underside)

BOLT_PCD = 103.0          # flange bolt circle diameter
BOLT_D = 7.0              # flange bolt hole diameter
BOLT_N = 8                # number of flange bolt holes

SLOT_ABOVE_FLANGE = 16.25 # centre of horizontal relief slot above flange
SLOT_T = 1.6              # relief slot thickness
SLIT_W = 3.0              # vertical clamp slit width

SCREW_X = 30.0            # clamp screw axis offset from bore axis
SCREW_BELOW_TOP = 10.4    # clamp screw axis depth below hub top
SCREW_HOLE_D = 8.0        # screw clearance hole
CB_D = 14.0               # screw-head counterbore diameter
CB_FLOOR_Y = 7.0          # counterbore floor position (+Y side)

POCKET_W = 15.6           # square nut-access pocket (-Y side)
POCKET_WALL_Y = -13.9     # pocket back wall (carries the nut recess)
NUT_AF = 12.5             # hex nut across flats
NUT_DEPTH = 6.0           # hex recess depth

SEAM_ANGLE = 180.0        # park cylinder seams on the back (-X) side

# ---------------- derived values ----------------
TOP_Z = FLANGE_T + HUB_H
SLOT_Z = FLANGE_T + SLOT_ABOVE_FLANGE
SCREW_Z = TOP_Z - SCREW_BELOW_TOP
BIG = 4.0 * FLANGE_D      # size of "infinite" cutting tools


def y_cylinder(x, z, d, y_start, y_end):
    """Cylinder of diameter d along the Y axis, from y_start to y_end."""
    lo, hi = min(y_start, y_end), max(y_start, y_end)
    return (cq.Workplane("XZ", origin=(0, hi, 0))   # XZ normal is -Y
            .center(x, z).circle(d / 2.0).extrude(hi - lo))


# ---------------- base body: flange + hub ----------------
flange = cq.Workplane("XY").circle(FLANGE_D / 2.0).extrude(FLANGE_T)
hub = (cq.Workplane("XY").workplane(offset=FLANGE_T)
       .circle(HUB_D / 2.0).extrude(HUB_H))
body = flange.union(hub).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# blind shaft bore from the top
bore = (cq.Workplane("XY").workplane(offset=BORE_BOTTOM_Z)
        .circle(BORE_D / 2.0).extrude(TOP_Z - BORE_BOTTOM_Z + 1.0))
body = body.cut(bore)

# flange bolt holes on the bolt circle (one on +X, equally spaced)
holes = (cq.Workplane("XY").workplane(offset=-1.0)
         .polarArray(BOLT_PCD / 2.0, 0, 360, BOLT_N)
         .circle(BOLT_D / 2.0).extrude(FLANGE_T + 2.0))
body = body.cut(holes)

# ---------------- clamp features ----------------
# horizontal relief slot through the whole +X half of the hub
slot = (cq.Workplane("XY")
        .box(BIG, BIG, SLOT_T, centered=(False, True, True))
        .translate((0, 0, SLOT_Z)))
body = body.cut(slot)

# vertical clamp slit on +X, from the relief slot up through the top
slit = (cq.Workplane("XY")
        .box(BIG, SLIT_W, TOP_Z - SLOT_Z + 1.0, centered=(False, True, False))
        .translate((0, 0, SLOT_Z)))
body = body.cut(slit)

# square nut-access pocket cut in from the -Y side, centred on the screw
pocket = (cq.Workplane("XY")
          .box(BIG, BIG, POCKET_W, centered=(False, False, True))
          .translate((SCREW_X - POCKET_W / 2.0, POCKET_WALL_Y - BIG, SCREW_Z)))
body = body.cut(pocket)

# hex nut recess in the pocket back wall (corners pointing up/down)
nut = (cq.Workplane("XZ", origin=(0, POCKET_WALL_Y - 1.0, 0))
       .center(SCREW_X, SCREW_Z)
       .polygon(6, NUT_AF / math.cos(math.radians(30)))
       .extrude(-(NUT_DEPTH + 1.0))          # towards +Y
       .rotate((SCREW_X, 0, SCREW_Z), (SCREW_X, 1, SCREW_Z), 30))
body = body.cut(nut)

# screw clearance hole straight through both clamp jaws
body = body.cut(y_cylinder(SCREW_X, SCREW_Z, SCREW_HOLE_D, -BIG, BIG))

# screw-head counterbore from the +Y side
body = body.cut(y_cylinder(SCREW_X, SCREW_Z, CB_D, CB_FLOOR_Y, BIG))

result = body
